import cadquery as cq

# ---------------------------------------------------------------
# Rectangular cover / mounting plate with rounded corners and four
# tapped corner holes (threads modelled as plain through holes).
# Plate stands upright in the XZ plane, thickness along Y.
# ---------------------------------------------------------------

# Driving dimensions (mm)
WIDTH = 50.0         # plate width  (X)
HEIGHT = 118.0       # plate height (Z)
THICK = 7.5          # plate thickness (Y)
CORNER_R = 8.5       # outline corner radius
HOLE_D = 5.9         # tapped hole nominal diameter (M6, plain)
HOLE_INSET_X = 10.4  # hole centre from left/right edges
HOLE_INSET_Z = 10.5  # hole centre from top/bottom edges

VIEW = {"azimuth": 45, "elevation": 26}

hx = WIDTH / 2.0 - HOLE_INSET_X
hz = HEIGHT / 2.0 - HOLE_INSET_Z
hole_pts = [(-hx, -hz), (hx, -hz), (-hx, hz), (hx, hz)]

# Base plate: rounded rectangle extruded symmetrically about XZ plane
plate = (
    cq.Workplane("XZ")
    .sketch()
    .rect(WIDTH, HEIGHT)
    .vertices()
    .fillet(CORNER_R)
    .finalize()
    .extrude(THICK / 2.0, both=True)
)

# Four through holes, drilled from the front (-Y) face
result = (
    plate.faces("<Y")
    .workplane(centerOption="CenterOfBoundBox")
    .pushPoints(hole_pts)
    .hole(HOLE_D)
)
